"""Tapered control knob: frustum about X (large end -X), 8 flat-floored grip pockets
with rounded rims, a blind bore in the large end and a pointer slot in the small end."""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 37.9            # overall length along X
R1 = 20.0           # radius of large end (-X)
R2 = 15.0           # radius of small end (+X)
FIL_BIG = 1.0       # edge round at large end
FIL_SMALL = 1.2     # edge round at small end

HOLE_D = 15.7       # blind bore in the large end face
HOLE_DEPTH = 20.0

N_POCKETS = 8       # grip pockets around the cone
POCKET_X0 = 0.231   # pocket start, fraction of L from the large end
POCKET_X1 = 0.765   # pocket end, fraction of L from the large end
POCKET_W = 5.1      # pocket width (tangential)
POCKET_FLOOR = 13.8 # distance of flat pocket floor from the axis
POCKET_FIL = 1.1    # rim round of pockets

SLOT_W = 5.0        # pointer slot in the small end face
SLOT_D = 2.45       # slot depth along X
SLOT_FIL = 1.1      # round on the slot bottom / end face edge

VIEW = {"azimuth": 45, "elevation": 26}

xa = -L / 2.0       # large end
xb = L / 2.0        # small end


# ---------------- main body: frustum about X ----------------
body = (
    cq.Workplane("XZ")
    .polyline([(xa, 0), (xa, R1), (xb, R2), (xb, 0)])
    .close()
    .revolve(360, (0, 0, 0), (1, 0, 0))
)
body = body.edges("%CIRCLE and <X").fillet(FIL_BIG)
body = body.edges("%CIRCLE and >X").fillet(FIL_SMALL)

# ---------------- bore in the large end ----------------
bore = (
    cq.Workplane("YZ", origin=(xa - 1.0, 0, 0))
    .circle(HOLE_D / 2.0)
    .extrude(HOLE_DEPTH + 1.0)
)
body = body.cut(bore)

# ---------------- grip pockets ----------------
px0 = xa + POCKET_X0 * L
px1 = xa + POCKET_X1 * L
pocket_h = R1 + 2.0 - POCKET_FLOOR
for i in range(N_POCKETS):
    ang = i * 360.0 / N_POCKETS
    cutter = (
        cq.Workplane("XY")
        .box(px1 - px0, POCKET_W, pocket_h, centered=(False, True, False))
        .translate((px0, 0, POCKET_FLOOR))
        .rotate((0, 0, 0), (1, 0, 0), ang)
    )
    body = body.cut(cutter)

# round the pocket rims: every edge the pockets left on the conical skin
solid = body.val()
cone_faces = [f for f in solid.Faces() if f.geomType() == "CONE"]
rim_edges = [
    e
    for f in cone_faces
    for e in f.Edges()
    if px0 - 0.3 < e.Center().x < px1 + 0.3
]
body = cq.Workplane("XY").newObject([solid.fillet(POCKET_FIL, rim_edges)])

# ---------------- pointer slot in the small end ----------------
slot = (
    cq.Workplane("XY")
    .box(SLOT_D + 1.0, SLOT_W, R1 + 2.0, centered=(False, True, False))
    .translate((xb - SLOT_D, 0, 0))
)
body = body.cut(slot)
body = body.edges(cq.selectors.NearestToPointSelector((xb, 0, 0))).fillet(SLOT_FIL)

result = body
